import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HEAD_D = 40.0          # knurled head outer diameter
HEAD_H = 6.85          # head thickness
KNURL_N = 23           # number of straight knurl grooves
KNURL_DEPTH = 1.35     # radial depth of each V groove
KNURL_ANGLE = 90.0     # included angle of V groove (deg)

THREAD_D = 20.0        # thread major diameter
SHANK_L = 23.85        # threaded shank length above head
THREAD_TURNS = 10      # thread turns over the shank length
PITCH = SHANK_L / THREAD_TURNS   # thread pitch (~2.4)
THREAD_PHASE = 0.55    # crest height above head face at +X (mod pitch)
CORE_SEAM_ANGLE = 90.0 # where the root cylinder's seam edge is placed (deg)

# ---------------- derived ----------------
R_HEAD = HEAD_D / 2.0
R_MAJ = THREAD_D / 2.0
H_FUND = math.sqrt(3.0) / 2.0 * PITCH          # fundamental triangle height
THREAD_DEPTH = 5.0 / 8.0 * H_FUND              # ISO basic thread depth
R_MIN = R_MAJ - THREAD_DEPTH
Z_TOP = HEAD_H + SHANK_L

# ---------------- knurled head ----------------
head = cq.Workplane("XY").circle(R_HEAD).extrude(HEAD_H)

# one V groove (triangular prism through the head), apex on the +X axis
half = math.radians(KNURL_ANGLE / 2.0)
ext = 1.0                                   # clearance outside the rim
apex_r = R_HEAD - KNURL_DEPTH
w = (KNURL_DEPTH + ext) * math.tan(half)
groove = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .polyline([(apex_r, 0.0), (R_HEAD + ext, w), (R_HEAD + ext, -w)])
    .close()
    .extrude(HEAD_H + 2.0)
    .val()
)
# polar pattern of grooves, offset half a pitch so a land sits on +X
step = 360.0 / KNURL_N
grooves = [
    groove.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), (k + 0.5) * step)
    for k in range(KNURL_N)
]
head = head.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(grooves)))

# ---------------- threaded shank ----------------
# thread ridge: ISO basic trapezoid (crest P/8, 60 deg flanks) swept along a
# right-hand helix; the flanks are continued below the minor radius so the
# ridge overlaps the core cleanly.
overlap = 0.3
crest_half = PITCH / 16.0             # half crest width at major radius
tan30 = math.tan(math.radians(30.0))
r_in = R_MIN - overlap
base_half = crest_half + (R_MAJ - r_in) * tan30
z_start = HEAD_H + THREAD_PHASE - PITCH   # first turn starts buried in the head
profile = cq.Wire.makePolygon(
    [
        cq.Vector(r_in, 0, z_start - base_half),
        cq.Vector(R_MAJ, 0, z_start - crest_half),
        cq.Vector(R_MAJ, 0, z_start + crest_half),
        cq.Vector(r_in, 0, z_start + base_half),
    ],
    close=True,
)
n_turns = int(math.ceil((Z_TOP + PITCH - z_start) / PITCH))
helix = cq.Wire.makeHelix(PITCH, n_turns * PITCH, r_in, center=cq.Vector(0, 0, z_start))
ridge = cq.Solid.sweep(profile, [], helix, makeSolid=True, isFrenet=True)

# core bar at the minor diameter; it fully encloses the ridge in Z so the
# boolean only has to resolve the cylinder/flank intersections
core_z0 = 0.5                         # core starts buried inside the head
core_top = z_start + (n_turns + 1) * PITCH
core = cq.Solid.makeCylinder(R_MIN, core_top - core_z0, cq.Vector(0, 0, core_z0))
# turn the cylinder's parametric seam to +Y (keeps seam edges off the front)
core = core.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), CORE_SEAM_ANGLE)
threaded = core.fuse(ridge)

# robustness guard: if the one-piece boolean silently dropped the ridge, rebuild
# the thread from stacked single-turn sweeps (same geometry, seam at 0 deg)
if not (core.Volume() + 1.0 < threaded.Volume() < core.Volume() + ridge.Volume() - 1.0):
    one = cq.Solid.sweep(
        profile, [], cq.Wire.makeHelix(PITCH, PITCH, r_in, center=cq.Vector(0, 0, z_start)),
        makeSolid=True, isFrenet=True,
    )
    threaded = core.fuse(*[one.translate(cq.Vector(0, 0, k * PITCH)) for k in range(n_turns)])

# trim the threaded bar to the shank length (flat top face)
envelope = cq.Solid.makeCylinder(R_MAJ + 0.5, Z_TOP - core_z0, cq.Vector(0, 0, core_z0))
shank = threaded.intersect(envelope)

result = head.union(cq.Workplane("XY").add(shank)).clean()

VIEW = {"azimuth": 45, "elevation": 26}
